import math
import cadquery as cq

# =====================================================================
#  Snap-in trim ring: flat flange ring with an inner chamfer and two
#  diametrically opposed clip legs (concave inner relief, barb tooth,
#  blind screw hole from below).
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0        # flange / leg outer radius
R_BORE = 40.4       # flange bore radius
T_FLANGE = 6.9      # flange thickness
CH_W = 2.8          # top inner chamfer, radial width
CH_H = 2.5          # top inner chamfer, height
H_LEG = 34.9        # leg height below the flange (leg bottoms at z = 0)

# leg plan outline at the leg foot (z = 0), for the leg on the -Y side
LEG_XO = 13.2               # +X / -X outer corners of the leg
LEG_B = (10.9, 39.2)        # kink point of the +X side (x, |y|)
LEG_IN_Y = 31.4             # radial position of the flat inner face
LEG_IN_XP = 6.7             # +X end of the flat inner face
LEG_XN_AT_B = -10.9         # -X side passes through (LEG_XN_AT_B, -LEG_B[1])
FIL_IN = 6.9                # round, -X inner vertical edge
FIL_OUT = 4.7               # round, -X outer vertical edge
FIL_KINK = 8.0              # round at the kink of the +X side

# the inner part of the leg sides tapers inward toward the flange
Z_TAPER = 13.0              # below this height the -X side is straight
TAPER_XP = 3.0              # +X side kink pulled in at the top (linear in z)
TAPER_XN = 4.6              # -X rounded corner shifted in at the top

# concave relief on the inside of the legs: arc of radius RELIEF_R,
# tangent to the flange bore at the flange underside, revolved about Z
RELIEF_R = 30.0

# barb / tooth at the foot of each leg
TOOTH_W = 9.2
TOOTH_TIP_Y = 22.7
TOOTH_TOP_Z = 12.6
TOOTH_TIP_Z = 2.1
TOOTH_BOT_Z = 1.1

# blind screw hole in each leg (from the foot up to the flange)
HOLE_R = 4.65
HOLE_C = 40.0

Z_FT = H_LEG + T_FLANGE


# ---------------- helpers ----------------
def _unit(v):
    n = math.hypot(v[0], v[1])
    return (v[0] / n, v[1] / n)


def _leg_frame():
    """Points of the leg outline that are shared by foot and top sections."""
    ya = math.sqrt(R_OUT**2 - LEG_XO**2)
    A = (LEG_XO, -ya)                                   # +X outer corner
    C = (LEG_IN_XP, -LEG_IN_Y)                          # +X inner corner
    # -X side line: through P0 = (-LEG_XO, -ya) and (LEG_XN_AT_B, -LEG_B[1])
    P0 = (-LEG_XO, -ya)
    P1 = (LEG_XN_AT_B, -LEG_B[1])
    u = _unit((P1[0] - P0[0], P1[1] - P0[1]))          # inward along the side
    # inner corner with the flat inner face y = -LEG_IN_Y, rounded
    s = (-LEG_IN_Y - P0[1]) / u[1]
    K = (P0[0] + s * u[0], -LEG_IN_Y)
    theta = math.acos(-u[0])                            # interior angle at K
    t = FIL_IN / math.tan(theta / 2.0)
    D = (K[0] + t, K[1])
    E = (K[0] - t * u[0], K[1] - t * u[1])
    cD = (D[0], D[1] - FIL_IN)
    # pivot of the tapered -X side: just inside the tangent point of the
    # outer round (round tangent to the side line and to R_OUT)
    n = (u[1], -u[0])
    lo, hi = -20.0, 20.0
    for _ in range(100):
        mid = 0.5 * (lo + hi)
        c = (P0[0] + mid * u[0] + FIL_OUT * n[0], P0[1] + mid * u[1] + FIL_OUT * n[1])
        if math.hypot(*c) > R_OUT - FIL_OUT:
            lo = mid
        else:
            hi = mid
    Q = (P0[0] + (lo + 1.0) * u[0], P0[1] + (lo + 1.0) * u[1])
    # points outside the ring used to close the outline (trimmed by R_OUT)
    ext = 4.0
    Pf = (P0[0] - ext * u[0], P0[1] - ext * u[1])
    ta = _unit((A[0] - LEG_B[0], A[1] + LEG_B[1]))      # +X side, outward
    Af = (A[0] + ext * ta[0], A[1] + ext * ta[1])
    y_far = min(Pf[1], Af[1]) - 2.0
    return dict(A=A, C=C, D=D, E=E, cD=cD, P0=P0, Q=Q, Pf=Pf, Af=Af, y_far=y_far)


def _round_corner(p_prev, p, p_next, r):
    """Tangent points and arc mid point of a round of radius r at corner p."""
    u1 = _unit((p_prev[0] - p[0], p_prev[1] - p[1]))
    u2 = _unit((p_next[0] - p[0], p_next[1] - p[1]))
    ang = math.acos(max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1])))
    t = r / math.tan(ang / 2.0)
    t1 = (p[0] + t * u1[0], p[1] + t * u1[1])
    t2 = (p[0] + t * u2[0], p[1] + t * u2[1])
    bis = _unit((u1[0] + u2[0], u1[1] + u2[1]))
    dc = r / math.sin(ang / 2.0)
    c = (p[0] + dc * bis[0], p[1] + dc * bis[1])
    m = (c[0] - r * bis[0], c[1] - r * bis[1])
    return t1, m, t2


def _arc_mid(center, r, p, q):
    """Mid point of the short arc p->q about center."""
    a1 = math.atan2(p[1] - center[1], p[0] - center[0])
    a2 = math.atan2(q[1] - center[1], q[0] - center[0])
    da = (a2 - a1 + math.pi) % (2 * math.pi) - math.pi
    am = a1 + da / 2.0
    return (center[0] + r * math.cos(am), center[1] + r * math.sin(am))


def _section(z, b_mid, dx_n):
    """Closed outline of the leg at height z (wire), oversize at the outer side.

    b_mid : kink point of the +X side
    dx_n  : shift (+X) of the rounded -X inner corner
    """
    f = _leg_frame()
    A, C, P0, Pf, Af = f["A"], f["C"], f["P0"], f["Pf"], f["Af"]
    D = (f["D"][0] + dx_n, f["D"][1])
    E = (f["E"][0] + dx_n, f["E"][1])
    cD = (f["cD"][0] + dx_n, f["cD"][1])
    mDE = _arc_mid(cD, FIL_IN, D, E)
    t1, mk, t2 = _round_corner(A, b_mid, C, FIL_KINK)
    wp = (
        cq.Workplane("XY", origin=(0, 0, z))
        .moveTo(*Af)
        .lineTo(*A)
        .spline(
            [t1, mk, t2, C],
            tangents=[_unit((b_mid[0] - A[0], b_mid[1] - A[1])),
                      _unit((C[0] - b_mid[0], C[1] - b_mid[1]))],
            includeCurrent=True,
        )
        .lineTo(*D)
        .threePointArc(mDE, E)
        .lineTo(*f["Q"])
        .lineTo(*P0)
        .lineTo(*Pf)
        .lineTo(Pf[0], f["y_far"])
        .lineTo(Af[0], f["y_far"])
        .close()
    )
    return wp.wire().val()


def make_leg():
    """Clip leg on the -Y side of the ring."""
    f = _leg_frame()
    w_foot = _section(0.0, (LEG_B[0], -LEG_B[1]), 0.0)
    w_mid = _section(Z_TAPER, (LEG_B[0] - TAPER_XP * Z_TAPER / H_LEG, -LEG_B[1]), 0.0)
    w_top = _section(H_LEG, (LEG_B[0] - TAPER_XP, -LEG_B[1]), TAPER_XN)
    body = cq.Solid.makeLoft([w_foot, w_mid, w_top], False)
    cyl = cq.Solid.makeCylinder(R_OUT, H_LEG)
    leg = cq.Workplane("XY").add(body.intersect(cyl))
    # round the -X outer vertical edge of the leg
    leg = leg.edges(
        cq.selectors.NearestToPointSelector((f["P0"][0], f["P0"][1], 0.5 * H_LEG))
    ).fillet(FIL_OUT)
    # concave relief on the inner face (revolved arc tangent to the bore)
    rc = R_BORE - RELIEF_R
    a_end = math.radians(-60.0)
    p_mid = (rc + RELIEF_R * math.cos(a_end / 2), H_LEG + RELIEF_R * math.sin(a_end / 2))
    p_end = (rc + RELIEF_R * math.cos(a_end), H_LEG + RELIEF_R * math.sin(a_end))
    relief = (
        cq.Workplane("XZ")
        .moveTo(0, H_LEG + 5.0)
        .lineTo(R_BORE, H_LEG + 5.0)
        .lineTo(R_BORE, H_LEG)
        .threePointArc(p_mid, p_end)
        .lineTo(0, p_end[1])
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
    )
    leg = leg.cut(relief)
    # barb tooth
    # (the sloped top runs on a little into the leg so it blends cleanly)
    slope = (TOOTH_TOP_Z - TOOTH_TIP_Z) / (LEG_IN_Y - TOOTH_TIP_Y)
    y_back = LEG_IN_Y + 1.5
    tooth = (
        cq.Workplane("YZ", origin=(-TOOTH_W / 2, 0, 0))
        .polyline([
            (-y_back, TOOTH_BOT_Z),
            (-TOOTH_TIP_Y, TOOTH_BOT_Z),
            (-TOOTH_TIP_Y, TOOTH_TIP_Z),
            (-y_back, TOOTH_TIP_Z + slope * (y_back - TOOTH_TIP_Y)),
        ])
        .close()
        .extrude(TOOTH_W)
    )
    leg = leg.union(tooth)
    return leg


# ---------------- flange: disc with a chamfered bore ----------------
# (the outer cylinder is turned half a turn so that its seam sits at -X,
#  the bore/chamfer seam is turned to 45 deg)
disc = (
    cq.Workplane("XY")
    .workplane(offset=H_LEG)
    .circle(R_OUT)
    .extrude(T_FLANGE)
    .rotate((0, 0, 0), (0, 0, 1), 180)
)
bore = (
    cq.Workplane("XZ")
    .polyline([
        (0.0, H_LEG - 1.0),
        (R_BORE, H_LEG - 1.0),
        (R_BORE, Z_FT - CH_H),
        (R_BORE + CH_W, Z_FT),
        (R_BORE + CH_W, Z_FT + 1.0),
        (0.0, Z_FT + 1.0),
    ])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), 45)
)
flange = disc.cut(bore)

leg_front = make_leg()
leg_back = leg_front.mirror("XZ")

body = flange.union(leg_front).union(leg_back)

# blind screw holes from the leg feet up to the flange underside
for sy in (-1, 1):
    hole = (
        cq.Workplane("XY")
        .center(0, sy * HOLE_C)
        .circle(HOLE_R)
        .extrude(H_LEG)
    )
    body = body.cut(hole)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
